import math
import cadquery as cq

# ---------------------------------------------------------------
# Finned hemispherical end-cap ("SIO CPG") with bolted flange
# Origin: centre of the flange back face.  Dome points to -Y.
# ---------------------------------------------------------------
R = 120.0                 # flange / fin outer radius
T_EDGE = 0.080 * R        # flange thickness at the outer rim
T_PLAT = 0.131 * R        # level of the flat ring around the dome / pad tops
DOME_C = -0.007 * R       # y of the dome sphere centre
DOME_RO = 0.74 * R        # dome outer radius
DOME_RI = 0.60 * R        # dome inner radius (hollow)
FIL_R = 0.0               # optional fillet between flat ring and dome (0 = sharp)
FIN_T = 0.075 * R         # fin thickness
RING_RO = 0.68 * R        # back lip outer radius
RING_RI = 0.645 * R       # back lip inner radius
RING_H = 0.053 * R        # back lip height
NOTCH_ANGLES = [53.0, 127.0, 233.0, 307.0]
NOTCH_W = 11.5            # notch angular width (deg)
N_BOLTS = 6
BOLT_PCD_R = 0.895 * R     # bolt circle radius
BOLT_START = 15.0         # angle of first bolt (deg, from +X toward +Z)
BOLT_D = 0.075 * R        # bolt hole diameter
HEX_AF = 0.128 * R        # hex nut-trap pocket across flats
HEX_DEPTH = 0.045 * R     # hex pocket depth below the pad top
PAD_RT = 0.094 * R        # pad top outline radius around the nut
PAD_DRAFT = 1.0           # pad wall slope (horizontal per vertical)
PAD_U_IN = 0.66 * R       # pad inner end (buried in the dome)
PAD_TIP_RHO = 0.765 * R   # outer radius of the flat ring (pad wing tips)
POCK_TIP_U = 0.752 * R    # pad side lines pass through these points
POCK_TIP_V = 0.139 * R
FIN_HOLE_D = 0.085 * R    # lanyard hole in the vertical fin
FIN_HOLE_Y = -0.185 * R
FIN_HOLE_Z = -0.85 * R
TEXT = "SIO CPG"
TEXT_ANGLES = [74.5, 65.0, 56.0, None, 40.0, 29.0, 16.5]
TEXT_Y = -0.228 * R       # text centre line (axial)
TEXT_SIZE = 0.200 * R     # font size
TEXT_DEPTH = 0.012 * R    # engraving depth

# ---------------------------------------------------------------
# main body of revolution: flange + conical collar + dome
# profile in (rho, y) -> sketch on XY plane (x=rho), revolve about Y
# ---------------------------------------------------------------
rho_j = math.sqrt(DOME_RO ** 2 - (-T_PLAT - DOME_C) ** 2)   # sharp junction radius


def _v(a, b):
    return (a[0] - b[0], a[1] - b[1])


def _n(a):
    l = math.hypot(a[0], a[1])
    return (a[0] / l, a[1] / l)


# collar: cone from the flange rim up to a narrow flat ring around the
# dome; optional concave fillet between that ring and the dome
P_A = (PAD_TIP_RHO, -T_PLAT)           # outer edge of the flat ring
P_J = (rho_j, -T_PLAT)
dL = _n(_v(P_A, P_J))                    # along the cone, outward
nL = (dL[1], -dL[0])                     # cone normal (toward -Y, outside)
O_d = (0.0, DOME_C)
if FIL_R > 0:
    # centre c = J + rf*n + s*d with |c - O_d| = r_d + rf
    bx = P_J[0] + FIL_R * nL[0] - O_d[0]
    by = P_J[1] + FIL_R * nL[1] - O_d[1]
    qb = 2 * (bx * dL[0] + by * dL[1])
    qc = bx * bx + by * by - (DOME_RO + FIL_R) ** 2
    s_f = (-qb + math.sqrt(qb * qb - 4 * qc)) / 2
    c_f = (P_J[0] + FIL_R * nL[0] + s_f * dL[0], P_J[1] + FIL_R * nL[1] + s_f * dL[1])
    T1 = (c_f[0] - FIL_R * nL[0], c_f[1] - FIL_R * nL[1])
    u2 = _n(_v(c_f, O_d))
    T2 = (O_d[0] + DOME_RO * u2[0], O_d[1] + DOME_RO * u2[1])
    bis = _n(((T1[0] - c_f[0]) + (T2[0] - c_f[0]), (T1[1] - c_f[1]) + (T2[1] - c_f[1])))
    F_mid = (c_f[0] + FIL_R * bis[0], c_f[1] + FIL_R * bis[1])
else:
    T1 = T2 = P_J
    F_mid = None


# nut pads: flat top, coplanar with the narrow flat ring around the dome
T_PAD = T_PLAT
a_2 = math.atan2(T2[1] - DOME_C, T2[0])
a_m = (a_2 - math.pi / 2) / 2.0
mid = (DOME_RO * math.cos(a_m), DOME_C + DOME_RO * math.sin(a_m))
tip = (0.0, DOME_C - DOME_RO)

prof = (
    cq.Workplane("XY")
    .moveTo(0, 0)
    .lineTo(R + 3.0, 0)
    .lineTo(R + 3.0, -T_EDGE)
    .lineTo(R, -T_EDGE)
    .lineTo(PAD_TIP_RHO, -T_PLAT)
    .lineTo(*T1)
)
if F_mid is not None:
    prof = prof.threePointArc(F_mid, T2)
body = prof.threePointArc(mid, tip).close().revolve(360, (0, 0, 0), (0, 1, 0))

# ---------------------------------------------------------------
# crossed fins: half discs (radius R) in the x=0 and z=0 planes; their
# rims lie on one sphere of radius R about the origin
# ---------------------------------------------------------------
fin_ball = cq.Workplane("XY").add(cq.Solid.makeSphere(R, cq.Vector(0, 0, 0), angleDegrees1=-90, angleDegrees2=90))
fin_h = (
    cq.Workplane("XY")
    .box(2 * R + 2, R, FIN_T, centered=(True, False, True))
    .translate((0, -R - 1.0, 0))
    .intersect(fin_ball)
)
fin_v = (
    cq.Workplane("XY")
    .box(FIN_T, R, 2 * R + 2, centered=(True, False, True))
    .translate((0, -R - 1.0, 0))
    .intersect(fin_ball)
)
fins = fin_h.union(fin_v, clean=False)


# ---------------------------------------------------------------
# raised nut pads: teardrop platforms on the conical collar, flat top
# level with the ring around the dome, 45 deg drafted side walls,
# trimmed flush with the flange rim; each has a hex nut trap + bolt hole.
# local frame (pad on +X axis): u radial (=x), v tangential (=z)
# ---------------------------------------------------------------
def tangent_point(px, py, cx, cy, r, side):
    dx, dy = px - cx, py - cy
    d = math.hypot(dx, dy)
    base = math.atan2(dy, dx)
    off = math.acos(r / d)
    ang = base + side * off
    return (cx + r * math.cos(ang), cy + r * math.sin(ang))


def line_at_u(p, q, u):
    t = (u - p[0]) / (q[0] - p[0])
    return (u, p[1] + t * (q[1] - p[1]))


def pad_wire(d, y):
    """pad outline offset outward by d, as a wire in plane y"""
    uc = BOLT_PCD_R
    tipA = (POCK_TIP_U, POCK_TIP_V)
    tipB = (POCK_TIP_U, -POCK_TIP_V)
    tA = tangent_point(tipA[0], tipA[1], uc, 0.0, PAD_RT, -1)
    tB = tangent_point(tipB[0], tipB[1], uc, 0.0, PAD_RT, +1)
    iA = line_at_u(tA, tipA, PAD_U_IN)
    iB = line_at_u(tB, tipB, PAD_U_IN)
    # offset: side lines move outward (radially from nut for tangents)
    def rad(p):
        vx, vy = p[0] - uc, p[1]
        n = math.hypot(vx, vy)
        return (p[0] + vx / n * d, p[1] + vy / n * d)
    tA2, tB2 = rad(tA), rad(tB)
    # proper offset of the inner corners: shift along side-line normal,
    # then slide along the line to u = PAD_U_IN - d
    oA = (iA[0] + (tA2[0] - tA[0]), iA[1] + (tA2[1] - tA[1]))
    oB = (iB[0] + (tB2[0] - tB[0]), iB[1] + (tB2[1] - tB[1]))
    iA2 = line_at_u(tA2, oA, PAD_U_IN - d)
    iB2 = line_at_u(tB2, oB, PAD_U_IN - d)
    far = (uc + PAD_RT + d, 0.0)

    def W(p):
        return cq.Vector(p[0], y, p[1])

    e1 = cq.Edge.makeLine(W(iA2), W(tA2))
    e2 = cq.Edge.makeThreePointArc(W(tA2), W(far), W(tB2))
    e3 = cq.Edge.makeLine(W(tB2), W(iB2))
    e4 = cq.Edge.makeLine(W(iB2), W(iA2))
    return cq.Wire.assembleEdges([e1, e2, e3, e4])


y_base = -T_EDGE + 0.02 * R
pad_d = (T_PAD - (T_EDGE - 0.02 * R)) * PAD_DRAFT
pad_loft = cq.Solid.makeLoft([pad_wire(pad_d, y_base), pad_wire(0.0, -T_PAD)], True)
pad0 = cq.Workplane("XY").add(pad_loft)
# trimming tube: everything outside radius R in the flange zone
trim = (
    cq.Workplane("XZ", origin=(0, 2.0, 0))
    .circle(2 * R)
    .circle(R)
    .extrude(T_PLAT + 0.1 * R)
)

# hex nut trap recessed into each pad
hexpock0 = (
    cq.Workplane("XZ", origin=(0, -T_PAD + HEX_DEPTH, 0))
    .center(BOLT_PCD_R, 0)
    .polygon(6, HEX_AF / math.cos(math.pi / 6))
    .extrude(HEX_DEPTH + 2.0)
)
hole0 = (
    cq.Workplane("XZ", origin=(0, RING_H + 5, 0))
    .center(BOLT_PCD_R, 0)
    .circle(BOLT_D / 2)
    .extrude(T_PLAT + RING_H + 20)
)

bolt_angles = [BOLT_START + i * 360.0 / N_BOLTS for i in range(N_BOLTS)]
# rotation about +Y by -ang maps +X toward +Z by ang
for ang in bolt_angles:
    body = body.union(pad0.rotate((0, 0, 0), (0, 1, 0), -ang))
body = body.cut(trim)
for ang in bolt_angles:
    body = body.cut(hexpock0.rotate((0, 0, 0), (0, 1, 0), -ang))
for ang in bolt_angles:
    body = body.cut(hole0.rotate((0, 0, 0), (0, 1, 0), -ang))

# ---------------------------------------------------------------
# back lip with notches
# ---------------------------------------------------------------
ring = (
    cq.Workplane("XZ", origin=(0, 0, 0))
    .circle(RING_RO)
    .circle(RING_RI)
    .extrude(-RING_H)
)
for a in NOTCH_ANGLES:
    wdg = (
        cq.Workplane("XZ", origin=(0, RING_H + 1, 0))
        .moveTo(0, 0)
        .lineTo(2 * R * math.cos(math.radians(a - NOTCH_W / 2)),
                2 * R * math.sin(math.radians(a - NOTCH_W / 2)))
        .lineTo(2 * R * math.cos(math.radians(a + NOTCH_W / 2)),
                2 * R * math.sin(math.radians(a + NOTCH_W / 2)))
        .close()
        .extrude(RING_H + 1)
    )
    ring = ring.cut(wdg)
body = body.union(ring)

# ---------------------------------------------------------------
# hollow dome interior (sphere + cylinder through the flange)
# ---------------------------------------------------------------
cav = (
    cq.Workplane("XY")
    .moveTo(0, RING_H + 5)
    .lineTo(DOME_RI, RING_H + 5)
    .lineTo(DOME_RI, DOME_C)
    .threePointArc(
        (DOME_RI * math.cos(math.radians(-45)), DOME_C + DOME_RI * math.sin(math.radians(-45))),
        (0, DOME_C - DOME_RI),
    )
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 1, 0), -90)
)
# fins are fused without face merging so that the fin edges stay visible
# across their crossing (the rims share one sphere)
body = body.union(fins, clean=False)
body = body.cut(cav, clean=False)

# lanyard hole through the vertical fin
# (circle seam placed on the side of the bore hidden from the usual views)
fh_plane = cq.Plane(
    origin=(-FIN_T, FIN_HOLE_Y, FIN_HOLE_Z),
    xDir=(0, -0.823, 0.567),
    normal=(1, 0, 0),
)
fh = cq.Workplane(fh_plane).circle(FIN_HOLE_D / 2).extrude(2 * FIN_T)
body = body.cut(fh, clean=False)

# ---------------------------------------------------------------
# engraved lettering on the dome near its base (+X/+Z quadrant)
# ---------------------------------------------------------------
try:
    rho_t = math.sqrt(DOME_RO ** 2 - (TEXT_Y - DOME_C) ** 2)
    dome_ball = cq.Workplane("XY").add(
        cq.Solid.makeSphere(DOME_RO + 0.05, cq.Vector(0, DOME_C, 0), angleDegrees1=-90, angleDegrees2=90))
    for ch, ad in zip(TEXT, TEXT_ANGLES):
        if ad is None or ch == " ":
            continue
        a = math.radians(ad)
        n = cq.Vector(rho_t * math.cos(a), TEXT_Y - DOME_C, rho_t * math.sin(a)).normalized()
        p = cq.Vector(0, DOME_C, 0) + n * (DOME_RO + 1.0)
        xd = cq.Vector(math.sin(a), 0, -math.cos(a))
        # make xd orthogonal to n
        xd = (xd - n * xd.dot(n)).normalized()
        pl = cq.Plane(origin=p, xDir=xd, normal=n)
        letter = (
            cq.Workplane(pl)
            .text(ch, TEXT_SIZE, -(TEXT_DEPTH + 1.0), combine=False,
                  halign="center", valign="center", kind="bold")
        )
        letter = letter.intersect(dome_ball)
        body = body.cut(letter, clean=False)
except Exception:
    pass

result = body
